import math
import cadquery as cq

# V-groove rope pulley: axis along X, small hub boss on the -X side,
# D-shaped shaft bore from the hub side (small round bore at the +X end),
# and an off-axis rope hole drilled from the +X face that breaks out
# into the V groove (break-out edge rounded).

IN = 25.4  # inch -> mm

# ---- driving dimensions ----
D_OUT       = 2.000 * IN   # flange outer diameter
D_GROOVE    = 1.000 * IN   # V-groove bottom diameter
D_HUB       = 1.000 * IN   # hub boss diameter
L_HUB       = 0.100 * IN   # hub boss length
L_FL_L      = 0.200 * IN   # hub-side flange thickness
L_TAPER     = 0.300 * IN   # axial length of each V flank
L_FLAT      = 0.100 * IN   # groove bottom flat width
L_FL_R      = 0.400 * IN   # outer flange thickness

D_BORE      = 0.330 * IN   # round through bore (seen at the +X face)
D_DBORE     = 0.625 * IN   # D-shaped shaft bore from the hub side
DFLAT_OFF   = 0.260 * IN   # axis -> D flat distance (flat on +Y side)
L_ROUND     = 0.200 * IN   # length of the small round bore at the +X end

D_PIN       = 0.300 * IN   # off-axis rope hole diameter
PIN_R       = 0.600 * IN   # radial position of the rope hole (+Z)
PIN_FILLET  = 1.0          # mm, rounding where the rope hole exits the V flank

# ---- axial stations (x along the pulley axis) ----
x_hub0 = -L_HUB
x0 = 0.0
x1 = x0 + L_FL_L
x2 = x1 + L_TAPER
x3 = x2 + L_FLAT
x4 = x3 + L_TAPER
x5 = x4 + L_FL_R

R_OUT = D_OUT / 2
R_G = D_GROOVE / 2
R_H = D_HUB / 2

# ---- revolved pulley body (half profile in XY, revolved about X) ----
profile = [
    (x_hub0, 0),
    (x_hub0, R_H),
    (x0, R_H),
    (x0, R_OUT),
    (x1, R_OUT),
    (x2, R_G),
    (x3, R_G),
    (x4, R_OUT),
    (x5, R_OUT),
    (x5, 0),
]
SEAM_ANGLE = -50.0  # deg, parks the revolve seam near the silhouette
body = (cq.Workplane("XY").polyline(profile).close()
        .revolve(360, (0, 0, 0), (1, 0, 0))
        .rotate((0, 0, 0), (1, 0, 0), SEAM_ANGLE))


def x_cyl(x_start, length, radius, cy=0.0, cz=0.0, seam_deg=90.0):
    """Cylinder along -X starting at x_start, axis through (y=cy, z=cz).
    seam_deg places the circle seam (angle from +Y towards +Z)."""
    a = math.radians(seam_deg)
    pl = cq.Plane(origin=(x_start, 0, 0),
                  xDir=(0, math.cos(a), math.sin(a)), normal=(-1, 0, 0))
    c = cq.Vector(0, cy, cz)
    return (cq.Workplane(pl)
            .center(c.dot(pl.xDir), c.dot(pl.yDir))
            .circle(radius).extrude(length))


# ---- round through bore ----
body = body.cut(x_cyl(x5 + 1.0, x5 - x_hub0 + 2.0, D_BORE / 2))

# ---- D-shaped shaft bore from the hub face (flat on +Y side) ----
rD = D_DBORE / 2
x_dend = x5 - L_ROUND                     # where the D bore stops
d_len = x_dend - x_hub0
dcyl = x_cyl(x_dend, d_len + 1.0, rD)
keep = (cq.Workplane("XY")
        .box(d_len + 2.0, 2 * rD + 2.0, 2 * rD + 2.0, centered=False)
        .translate((x_hub0 - 1.5, DFLAT_OFF - 2 * rD - 2.0, -rD - 1.0)))
body = body.cut(dcyl.intersect(keep))

# ---- off-axis rope hole: from the +X face to the groove-bottom edge ----
pin = x_cyl(x5 + 1.0, x5 + 1.0 - x2, D_PIN / 2, cz=PIN_R, seam_deg=225.0)
body = body.cut(pin)

# ---- round over the hole's break-out edge on the outer V flank ----
solid = body.solids().val()
eps = 0.05
exit_edges = [
    e for e in solid.Edges()
    if e.BoundingBox().zmin > 0.5 * R_G
    and e.BoundingBox().xmin > x3 - eps
    and e.BoundingBox().xmax > x3 + 0.5
    and e.BoundingBox().xmax < x4 - eps
]
if exit_edges and PIN_FILLET > 0:
    for r in (PIN_FILLET, PIN_FILLET * 0.95, PIN_FILLET * 1.05, PIN_FILLET * 0.9):
        try:
            filleted = solid.fillet(r, exit_edges)
            if filleted.isValid():
                solid = filleted
                break
        except Exception:
            pass

result = cq.Workplane("XY").add(solid)
